import math
import cadquery as cq

# ---------------------------------------------------------------
# Printer X-end (motor side) style part:
#   * base = two hexagonal-profile rod holders (rods along X) joined
#     by side walls, with a window between them
#   * hexagonal nut-trap column for the Z lead screw
#   * split (C-section) vertical bearing tube with lips and zip-tie rings
#   * NEMA17-style L-shaped motor plate with a foot and a diagonal brace
# Dimensions are given in drawing units "u" and scaled to mm by S.
# Axes: X to the right, Y to the back, Z up (plate faces -Y).
# ---------------------------------------------------------------
S = 0.28  # mm per drawing unit
YAW_DEG = 1.3            # the whole part sits turned slightly about the vertical axis
YAW_PIVOT = (63.5, 0.0)  # (x, y) of the pivot: front-left corner of the motor plate


def u(v):
    return v * S


# ---------------- base (rod holders) ----------------
BASE_X0, BASE_X1 = 21.5, 168.5
BASE_H = 56.6
ROD_Z = 24.0
BASE_PROFILE = [(41.0, 0), (38.5, ROD_Z), (56.5, BASE_H), (266.0, BASE_H), (280.0, ROD_Z), (276.5, 0)]
WIN_X0, WIN_X1 = 59.4, 108.0
WIN_PROFILE = [(96.6, -5), (96.6, ROD_Z), (82.6, BASE_H + 5), (240.5, BASE_H + 5),
               (222.5, ROD_Z), (222.5, -5)]
ROD_Y = (67.5, 250.8)
ROD_D = 29.0
ROD_END_X = 152.0          # blind rod holes, entered from the -X end
GAP_X0, GAP_Y0, GAP_Y1 = 151.8, 116.0, 200.9   # relief around the bearing tube foot

# ---------------- nut trap column ----------------
HEX_CX, HEX_CY = 41.1, 160.2
HEX_AF = 74.0
HEX_H = 145.5
NUT_AF = 48.5
NUT_DEPTH = 30.0
BOT_NUT_DEPTH = 30.0
BRIDGE = 1.5
SCREW_D = 31.0

# ---------------- bearing tube ----------------
TUBE_CX, TUBE_CY = 147.6, 160.5
TUBE_R = 36.4
TUBE_FLAT_X = TUBE_CX - 35.6   # flat -X side of the D-shaped outline
TUBE_H = 236.25
BORE_R = 29.9
LIP_X = TUBE_CX - 19.4     # lips: bore flattened on the -X side
LIPS = [(0.0, 7.0), (97.0, 104.0), (132.0, 141.0), (229.5, TUBE_H)]
SLOT_HALF_ANGLE = 42.0    # the C opens towards +X (radial wall ends)
TIE_R_IN, TIE_R_OUT = 32.5, 36.9
TIE_BANDS = [(60.0, 75.0), (167.0, 182.0)]

# ---------------- motor plate ----------------
PLATE_T = 33.0
MOTOR_C = (143.1, 113.4)   # motor axis (centre of the NEMA17 hole square)
HOLE_PITCH = 110.75        # 31 mm hole spacing
HOLE_D = 15.0
CB_D = 24.0                # screw-head clearance behind the plate
CB_Y1 = 49.5
CORNER_R = 23.75           # rounding around the lower holes
CLEAR_R = 49.5             # concave clearance for the motor boss
TOP_FILLET = 34.5          # blend of the clearance arc into the upright
PLATE_X0 = 175.5           # inner edge of the upright
PLATE_TOP = 205.0
SIDE_SAG = 5.0             # slight concavity of the plate's +X edge ...
SIDE_SPAN = (65.0, 165.0)  # ... between these heights
TWIST_Z = (164.0, 190.0)   # upright's back corner blends into the brace
HOLE_L = (MOTOR_C[0] - HOLE_PITCH / 2, MOTOR_C[1] - HOLE_PITCH / 2)
HOLE_BR = (MOTOR_C[0] + HOLE_PITCH / 2, MOTOR_C[1] - HOLE_PITCH / 2)
HOLE_TOP = (MOTOR_C[0] + HOLE_PITCH / 2, MOTOR_C[1] + HOLE_PITCH / 2)
PLATE_X1 = HOLE_BR[0] + CORNER_R

# foot under / behind the plate
LB_X0 = HOLE_L[0] - CORNER_R
LB_TOP = 57.6
LB_BACK_TOP_Y = 42.0
LB_BACK_BOT = (65.0, 12.6)
FOOT_RUN = 0.53           # foot front: setback in y per unit of drop below the plate edge
HUMP = 6.0                 # plate's lower edge rises between the two lower holes
HUMP_JOIN = 8.0            # degrees past the bottom of the hole roundings where it starts

# ---------------- brace ----------------
BAR_Z0, BAR_Z1 = 183.0, 205.0
BAR_SLOPE = 0.4865         # dX/dY of the brace (runs back and towards -X)
BAR_END_Y = 140.0


def prism_x(profile, x0, x1):
    """Polygon given in (Y, Z) extruded along +X from x0 to x1."""
    pts = [(u(y), u(z)) for (y, z) in profile]
    return (cq.Workplane("YZ", origin=(u(x0), 0, 0))
            .polyline(pts).close().extrude(u(x1 - x0)))


def cyl_z(cx, cy, r, z0, z1):
    return (cq.Workplane("XY", origin=(0, 0, u(z0))).center(u(cx), u(cy))
            .circle(u(r)).extrude(u(z1 - z0)))


def cyl_y(cx, cz, r, y0, y1):
    # XZ workplane normal is -Y, so a negative extrude goes towards +Y
    return (cq.Workplane("XZ", origin=(0, u(y0), 0)).center(u(cx), u(cz))
            .circle(u(r)).extrude(-u(y1 - y0)))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY", origin=(0, 0, u(z0)))
            .center(u((x0 + x1) / 2), u((y0 + y1) / 2))
            .rect(u(x1 - x0), u(y1 - y0)).extrude(u(z1 - z0)))


def hex_z(cx, cy, af, z0, z1):
    """Hexagonal prism with flats facing +-X (corners towards +-Y)."""
    r = af / math.sqrt(3)
    pts = [(u(cx + r * math.cos(math.radians(a))), u(cy + r * math.sin(math.radians(a))))
           for a in (30, 90, 150, 210, 270, 330)]
    return (cq.Workplane("XY", origin=(0, 0, u(z0)))
            .polyline(pts).close().extrude(u(z1 - z0)))


# ================= base =================
base = prism_x(BASE_PROFILE, BASE_X0, BASE_X1)
base = base.cut(prism_x(WIN_PROFILE, WIN_X0, WIN_X1))
base = base.cut(box(GAP_X0, BASE_X1 + 1, GAP_Y0, GAP_Y1, -1, BASE_H + 1))

# ================= nut trap column =================
hexcol = hex_z(HEX_CX, HEX_CY, HEX_AF, 0, HEX_H)

# ================= bearing tube (outer) =================
tube = cyl_z(TUBE_CX, TUBE_CY, TUBE_R, 0, TUBE_H).union(
    box(TUBE_FLAT_X, TUBE_CX, TUBE_CY - TUBE_R, TUBE_CY + TUBE_R, 0, TUBE_H))
tube = tube.intersect(box(TUBE_FLAT_X, TUBE_CX + 50, TUBE_CY - 50, TUBE_CY + 50, 0, TUBE_H))

# ================= motor plate =================
def plate_outline():
    """Key points of the L-shaped NEMA17 plate outline in the XZ plane."""
    mx, mz = MOTOR_C
    # blend between upright edge (x = PLATE_X0) and clearance circle
    rho = TOP_FILLET
    fx = PLATE_X0 + rho
    fz = mz + math.sqrt((CLEAR_R + rho) ** 2 - (fx - mx) ** 2)
    d = math.hypot(fx - mx, fz - mz)
    t1a = (PLATE_X0, fz)
    t1b = (mx + CLEAR_R * (fx - mx) / d, mz + CLEAR_R * (fz - mz) / d)
    a1 = math.atan2(t1a[1] - fz, t1a[0] - fx)
    a2 = math.atan2(t1b[1] - fz, t1b[0] - fx)
    while a2 - a1 > math.pi:
        a2 -= 2 * math.pi
    while a1 - a2 > math.pi:
        a2 += 2 * math.pi
    f_mid = (fx + rho * math.cos((a1 + a2) / 2), fz + rho * math.sin((a1 + a2) / 2))
    # straight tangent from the left boss to the clearance circle
    bx, bz = HOLE_L
    dxm, dzm = mx - bx, mz - bz
    L = math.hypot(dxm, dzm)
    base_ang = math.atan2(dxm, dzm)
    phi = math.asin((CORNER_R + CLEAR_R) / L) - base_ang
    nx, nz = math.sin(phi), math.cos(phi)
    t2a = (bx + CORNER_R * nx, bz + CORNER_R * nz)
    t2b = (mx - CLEAR_R * nx, mz - CLEAR_R * nz)
    # clearance arc mid point (lower right)
    ang_b = math.atan2(t1b[1] - mz, t1b[0] - mx)
    ang_e = math.atan2(t2b[1] - mz, t2b[0] - mx)
    if ang_e > ang_b:
        ang_e -= 2 * math.pi
    c_mid = (mx + CLEAR_R * math.cos((ang_b + ang_e) / 2), mz + CLEAR_R * math.sin((ang_b + ang_e) / 2))
    # boss arc mid point (from the tangent point round to the leftmost point)
    ab = math.atan2(t2a[1] - bz, t2a[0] - bx)
    b_mid = (bx + CORNER_R * math.cos((ab + math.pi) / 2), bz + CORNER_R * math.sin((ab + math.pi) / 2))
    o = dict(t1a=t1a, t1b=t1b, f_mid=f_mid, c_mid=c_mid, t2b=t2b, t2a=t2a, b_mid=b_mid)
    o.update(lower_outline_pts())
    return o


def lower_outline_pts():
    """Points of the plate's lower edge: left rounding, hump, right rounding."""
    bx, bz = HOLE_L
    rx, rz = HOLE_BR
    j = math.radians(90 - HUMP_JOIN)
    j1 = (bx + CORNER_R * math.cos(-j), bz - CORNER_R * math.sin(j))
    j2 = (rx - CORNER_R * math.cos(-j), rz - CORNER_R * math.sin(j))
    hump_top = ((j1[0] + j2[0]) / 2, bz - CORNER_R + HUMP)
    h = math.radians((90 - HUMP_JOIN) / 2)
    lb_mid = (bx + CORNER_R * math.cos(math.pi + h), bz + CORNER_R * math.sin(math.pi + h))
    rb_mid = (rx + CORNER_R * math.cos(-h), rz + CORNER_R * math.sin(-h))
    return dict(j1=j1, j2=j2, hump_top=hump_top, lb_left=(bx - CORNER_R, bz),
                lb_mid=lb_mid, rb_mid=rb_mid, r_side=(PLATE_X1, rz))


def U(p):
    return (u(p[0]), u(p[1]))


o = plate_outline()
plate = (cq.Workplane("XZ")
         .moveTo(*U((PLATE_X0, PLATE_TOP)))
         .lineTo(*U(o["t1a"]))
         .threePointArc(U(o["f_mid"]), U(o["t1b"]))
         .threePointArc(U(o["c_mid"]), U(o["t2b"]))
         .lineTo(*U(o["t2a"]))
         .threePointArc(U(o["b_mid"]), U(o["lb_left"]))
         .threePointArc(U(o["lb_mid"]), U(o["j1"]))
         .threePointArc(U(o["hump_top"]), U(o["j2"]))
         .threePointArc(U(o["rb_mid"]), U(o["r_side"]))
         .lineTo(*U((PLATE_X1, PLATE_TOP)))
         .close()
         .extrude(-u(PLATE_T)))
# slightly concave outer (+X) edge
half = (SIDE_SPAN[1] - SIDE_SPAN[0]) / 2.0
rho_s = (half ** 2 + SIDE_SAG ** 2) / (2 * SIDE_SAG)
plate = plate.cut(cyl_y(PLATE_X1 - SIDE_SAG + rho_s, (SIDE_SPAN[0] + SIDE_SPAN[1]) / 2, rho_s,
                        -1, PLATE_T + 1))

# back-right corner of the upright twists into the diagonal brace face
e = 2.0
zlo, zhi = TWIST_Z
bot = [(PLATE_X1 + 0.05, -e), (PLATE_X1 - 0.3, PLATE_T + e), (PLATE_X1 + 30, PLATE_T + e),
       (PLATE_X1 + 30, -e)]
top = [(PLATE_X1 + BAR_SLOPE * e, -e), (PLATE_X1 - BAR_SLOPE * (PLATE_T + e), PLATE_T + e),
       (PLATE_X1 + 30, PLATE_T + e), (PLATE_X1 + 30, -e)]
w_bot = cq.Wire.makePolygon([cq.Vector(u(x), u(y), u(zlo)) for x, y in bot], close=True)
w_top = cq.Wire.makePolygon([cq.Vector(u(x), u(y), u(zhi)) for x, y in top], close=True)
twist = cq.Workplane("XY").add(cq.Solid.makeLoft([w_bot, w_top], True))
above = (cq.Workplane("XY", origin=(0, 0, u(zhi - 0.01)))
         .polyline([U(p) for p in top]).close().extrude(u(PLATE_TOP - zhi + 5)))
plate = plate.cut(twist).cut(above)

# foot behind/below the plate: its front face is the plate's lower edge swept
# backwards and downwards (oblique prism), its back is sloped
foot = (cq.Workplane("YZ", origin=(u(LB_X0), 0, 0))
        .polyline([(0, 0), (u(LB_BACK_BOT[0]), 0), (u(LB_BACK_BOT[0]), u(LB_BACK_BOT[1])),
                   (u(LB_BACK_TOP_Y), u(LB_TOP)), (0, u(LB_TOP))]).close()
        .extrude(u(PLATE_X1 - LB_X0)))
lo = lower_outline_pts()
y_start = -1.0
dz = -y_start / FOOT_RUN          # lift the edge so the swept surface passes y=0 at the edge


def Ul(p):
    return (u(p[0]), u(p[1] + dz))


g = (cq.Workplane("XZ", origin=(0, u(y_start), 0))
     .moveTo(*Ul((LB_X0 - 5, HOLE_L[1])))
     .lineTo(*Ul(lo["lb_left"]))
     .threePointArc(Ul(lo["lb_mid"]), Ul(lo["j1"]))
     .threePointArc(Ul(lo["hump_top"]), Ul(lo["j2"]))
     .threePointArc(Ul(lo["rb_mid"]), Ul(lo["r_side"]))
     .lineTo(*Ul((PLATE_X1 + 5, HOLE_BR[1])))
     .lineTo(*Ul((PLATE_X1 + 5, -150)))
     .lineTo(*Ul((LB_X0 - 5, -150)))
     .close())
run = 90.0
sweep_vec = cq.Vector(0, u(run), -u(run / FOOT_RUN))
front_cut = cq.Solid.extrudeLinear(g.val(), [], sweep_vec)
foot = foot.cut(cq.Workplane("XY").add(front_cut))
plate = plate.union(foot)

# ================= brace =================
bar_pts = [(PLATE_X0, 0), (PLATE_X1, 0),
           (PLATE_X1 - BAR_SLOPE * BAR_END_Y, BAR_END_Y),
           (PLATE_X0 - BAR_SLOPE * BAR_END_Y, BAR_END_Y)]
bar = (cq.Workplane("XY", origin=(0, 0, u(BAR_Z0)))
       .polyline([(u(x), u(y)) for x, y in bar_pts]).close().extrude(u(BAR_Z1 - BAR_Z0)))
bar = bar.intersect(box(TUBE_FLAT_X, 260, -10, 300, BAR_Z0 - 5, BAR_Z1 + 5))

result = base.union(hexcol).union(tube).union(plate).union(bar)

# ================= cuts =================
# rod holes (teardrop, blind)
for ry in ROD_Y:
    r = ROD_D / 2
    tip = r * math.sqrt(2)
    td = (cq.Workplane("YZ", origin=(u(BASE_X0 - 1), 0, 0))
          .center(u(ry), u(ROD_Z)).circle(u(r)).extrude(u(ROD_END_X - BASE_X0 + 1)))
    tri = (cq.Workplane("YZ", origin=(u(BASE_X0 - 1), 0, 0))
           .polyline([(u(ry - r / math.sqrt(2)), u(ROD_Z + r / math.sqrt(2))),
                      (u(ry), u(ROD_Z + tip)),
                      (u(ry + r / math.sqrt(2)), u(ROD_Z + r / math.sqrt(2))),
                      (u(ry), u(ROD_Z))]).close()
           .extrude(u(ROD_END_X - BASE_X0 + 1)))
    result = result.cut(td).cut(tri)

# nut traps and lead-screw hole (bridged)
result = result.cut(hex_z(HEX_CX, HEX_CY, NUT_AF, HEX_H - NUT_DEPTH, HEX_H + 1))
result = result.cut(hex_z(HEX_CX, HEX_CY, NUT_AF, -1, BOT_NUT_DEPTH))
result = result.cut(cyl_z(HEX_CX, HEX_CY, SCREW_D / 2, BOT_NUT_DEPTH + BRIDGE, HEX_H - NUT_DEPTH + 1))

# bearing bore with retaining lips on the -X side
result = result.cut(cyl_z(TUBE_CX, TUBE_CY, BORE_R, -1, TUBE_H + 1))
for z0, z1 in LIPS:
    lip = cyl_z(TUBE_CX, TUBE_CY, BORE_R + 0.5, z0, z1).intersect(
        box(TUBE_FLAT_X - 1, LIP_X, TUBE_CY - 40, TUBE_CY + 40, z0, z1))
    result = result.union(lip)
# split opening towards +X
a = math.radians(SLOT_HALF_ANGLE)
Ls = 90.0
slot_pts = [(TUBE_CX, TUBE_CY),
            (TUBE_CX + Ls * math.cos(a), TUBE_CY - Ls * math.sin(a)),
            (TUBE_CX + Ls * math.cos(a), TUBE_CY + Ls * math.sin(a))]
slot = (cq.Workplane("XY", origin=(0, 0, -u(1)))
        .polyline([(u(x), u(y)) for x, y in slot_pts]).close().extrude(u(TUBE_H + 2)))
result = result.cut(slot)
# zip-tie rings
for z0, z1 in TIE_BANDS:
    ring = cyl_z(TUBE_CX, TUBE_CY, TIE_R_OUT, z0, z1).cut(
        cyl_z(TUBE_CX, TUBE_CY, TIE_R_IN, z0 - 1, z1 + 1))
    result = result.cut(ring)

# motor screw holes + head clearance
for hx, hz in (HOLE_TOP, HOLE_BR, HOLE_L):
    result = result.cut(cyl_y(hx, hz, HOLE_D / 2, -5, PLATE_T + 5))
for hx, hz in (HOLE_BR, HOLE_L):
    result = result.cut(cyl_y(hx, hz, CB_D / 2, PLATE_T, CB_Y1))

# final placement: small yaw about the vertical axis
result = result.rotate((u(YAW_PIVOT[0]), u(YAW_PIVOT[1]), 0),
                       (u(YAW_PIVOT[0]), u(YAW_PIVOT[1]), 1), YAW_DEG)
